import math
import cadquery as cq
from OCP.BRep import BRep_Tool
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.BRepOffsetAPI import BRepOffsetAPI_MakePipeShell
from OCP.Geom import Geom_BSplineSurface, Geom_TrimmedCurve
from OCP.GeomConvert import GeomConvert, GeomConvert_CompCurveToBSplineCurve

# ---------------------------------------------------------------------------
# Wheel fender (mudguard) with a bent sheet-metal mounting bracket on top.
# Frame: X = across the wheel, Y = rearwards, Z = up; the origin sits on the
# (virtual) wheel axle.  The rear half of the fender is a spheroidal dome
# swept about the axle (X axis); the front half is a straight tunnel that
# leaves the dome tangentially, rising towards the front, and whose section
# grows from the elliptical dome section to a fuller front edge section.
# ---------------------------------------------------------------------------

# --- fender shell -----------------------------------------------------------
A_X = 152.6          # half width of the dome section (ellipse semi axis, X)
B_R = 161.5          # crown radius of the fender section (radial semi axis)
W_F = 149.8          # half width of the front edge section (super-ellipse)
N_F = 2.48           # super-ellipse exponent of the fuller front edge section
T = 4.0              # wall thickness
R_MIN = 3.0          # sections are trimmed at this radius (keeps off the axle)
TILT = 11.3          # the forward tunnel rises at this angle (deg)
L_TUN = 124.0        # length of the forward tunnel
REV_END = 200.0      # dome swept to this angle (deg from +Z towards +Y)
CUT_M = -0.207       # rear lower edge of the skirts: z = CUT_M * y + CUT_C
CUT_C = -12.6
R_TB = 19.0          # lower edge of the tunnel skirts, radius above tunnel axis
Y_S = -22.0          # lower edge dips towards the axle from here (tunnel frame)
CORNER_R = 34.0      # rounded front lower corner of the skirts
BEAD_R = 4.5         # rolled bead along the front edge (tube radius)
HOLE_D = 6.5         # fastener hole diameter

# --- inner doubler (reinforcement on the inside of the crown) ---------------
DB_T = 2.5           # sheet thickness of doubler and strap
DB_W = 158.0         # width of the wide upper part
DB_Z = 117.0         # lower edge of the wide part (height above axle)
DB_F = 12.0          # the doubler reaches this far forward into the tunnel
ST_W = 50.0          # width of the strap running down the back
ST_Z0 = 137.0        # upper end of the strap
ST_Z = 45.0          # lower end of the strap

# --- bracket (bent sheet-metal tray on top) ----------------------------------
PL_W = 154.0         # plate width over the side flanges
PL_T = 3.0           # sheet thickness
PL_Z = 160.0         # top of the plate
PL_Y0 = -19.0        # front end of the plate
PL_Y1 = 161.6        # rear end of the plate (outside of the rear flange)
FL_Z = 117.0         # lower edge of the rear flange / free side flanges
BEND_R = 8.0         # outside bend radius
CORNER_PL = 16.0     # rear corner radius of the tray (plan view)
GUSSET_X = 35.0      # single gusset plate under the tray (right-hand side)

ct, st = math.cos(math.radians(TILT)), math.sin(math.radians(TILT))


# ------------------------------------------------------------ helpers -----
def tilt_pt(y, z):
    """untilted tunnel frame (y, z) -> final frame (y, z)."""
    return (y * ct + z * st, -y * st + z * ct)


def untilt_pt(y, z):
    return (y * ct - z * st, y * st + z * ct)


def r_of_x(x, a=A_X, b=B_R):
    return b * math.sqrt(max(0.0, 1.0 - (x / a) ** 2))


def x_of_r(r, a=A_X, b=B_R):
    return a * math.sqrt(max(0.0, 1.0 - (r / b) ** 2))


def r_sup(x, a=W_F, b=B_R, n=N_F):
    return b * max(0.0, 1.0 - abs(x / a) ** n) ** (1.0 / n)


def x_sup(r, a=W_F, b=B_R, n=N_F):
    return a * max(0.0, 1.0 - (r / b) ** n) ** (1.0 / n)


def to_bspline_curve(edge):
    return GeomConvert.CurveToBSplineCurve_s(
        Geom_TrimmedCurve(BRep_Tool.Curve_s(edge.wrapped, 0, 1), *edge._bounds()))


def refine(curve, n):
    """insert n-1 uniform knots (exact; gives swept skins an even
    parametrisation and therefore a clean tessellation)."""
    a, b = curve.FirstParameter(), curve.LastParameter()
    for k in range(1, n):
        curve.InsertKnot(a + (b - a) * k / n, 1, 1e-9, True)
    return cq.Edge(BRepBuilderAPI_MakeEdge(curve).Edge())


def ell_curve(a, b, rmin):
    """Elliptical section curve (right to left) above z = rmin (XZ plane)."""
    t = math.degrees(math.asin(rmin / b))
    e = cq.Edge.makeEllipse(a, b, cq.Vector(0, 0, 0), cq.Vector(0, -1, 0),
                            cq.Vector(1, 0, 0), t, 180.0 - t, 1)
    return refine(to_bspline_curve(e), 16), a * math.cos(math.radians(t))


def sup_curve(a, b, n, rmin, npts=33):
    """Super-ellipse |x/a|^n + |z/b|^n = 1 (right to left) above z = rmin, as
    one smooth interpolating B-spline."""
    t0 = math.asin((rmin / b) ** (n / 2.0))
    pts = []
    for k in range(npts):
        t = t0 + (math.pi - 2.0 * t0) * k / (npts - 1)
        c, s_ = math.cos(t), math.sin(t)
        pts.append(cq.Vector(a * math.copysign(abs(c) ** (2.0 / n), c), 0,
                             b * abs(s_) ** (2.0 / n)))
    pts[0] = cq.Vector(pts[0].x, 0, rmin)
    pts[-1] = cq.Vector(pts[-1].x, 0, rmin)
    return cq.Edge.makeSpline(pts), pts[0].x


def section_wire(outer, inner=None, rmin=R_MIN):
    """Closed section from an outer (and optional inner) curve whose ends lie
    on z = rmin; curves given as (edge, end x)."""
    eo, xo = outer
    if inner is None:
        edges = [eo, cq.Edge.makeLine(cq.Vector(-xo, 0, rmin), cq.Vector(xo, 0, rmin))]
    else:
        ei, xi = inner
        edges = [eo,
                 cq.Edge.makeLine(cq.Vector(-xo, 0, rmin), cq.Vector(-xi, 0, rmin)),
                 ei,
                 cq.Edge.makeLine(cq.Vector(xi, 0, rmin), cq.Vector(xo, 0, rmin))]
    return cq.Wire.assembleEdges(edges)


def dome_wire(a, b, t=None):
    return section_wire(ell_curve(a, b, R_MIN), None if t is None else ell_curve(a - t, b - t, R_MIN))


def front_wire(a, b, n, t=None):
    return section_wire(sup_curve(a, b, n, R_MIN),
                        None if t is None else sup_curve(a - t, b - t, n, R_MIN))


def crown_path(th_end, tunnel):
    """Crown line (untilted frame): optional straight lead-in of length
    `tunnel` along +Y ending at the crown point (0, 0, B_R), then an arc of
    radius B_R about the axle up to th_end; one exact B-spline edge."""
    p_j = cq.Vector(0, 0, B_R)
    th_m, th_e = math.radians(0.5 * th_end), math.radians(th_end)
    arc = cq.Edge.makeThreePointArc(p_j, cq.Vector(0, B_R * math.sin(th_m), B_R * math.cos(th_m)),
                                    cq.Vector(0, B_R * math.sin(th_e), B_R * math.cos(th_e)))
    curve = to_bspline_curve(arc)
    if tunnel > 0:
        comp = GeomConvert_CompCurveToBSplineCurve(
            to_bspline_curve(cq.Edge.makeLine(p_j - cq.Vector(0, tunnel, 0), p_j)))
        comp.Add(curve, 1e-6)
        curve = comp.BSplineCurve()
    return cq.Wire.assembleEdges([refine(curve, 24)])


def sweep(wire, th_end, tunnel=0.0):
    """Sweep a section (given at the junction plane y = 0) along the crown:
    a straight lead-in of length `tunnel` then the dome about the axle."""
    pipe = BRepOffsetAPI_MakePipeShell(crown_path(th_end, tunnel).wrapped)
    pipe.SetMode(False)                 # corrected Frenet (planar path)
    pipe.Add(wire.translate(cq.Vector(0, -tunnel, 0)).wrapped, False, False)
    pipe.SetMaxDegree(3)                # low degree skin -> robust booleans
    pipe.SetMaxSegments(100)
    pipe.Build()
    pipe.MakeSolid()
    return cq.Shape.cast(pipe.Shape())


def tunnel_loft(w_front, w_junction):
    """Ruled skin from the front edge section (y = -L_TUN) to the junction."""
    tun = cq.Solid.makeLoft([w_front.translate(cq.Vector(0, -L_TUN, 0)), w_junction], True)
    # the skin is linear along the rulings: add knots there (exact) so that it
    # tessellates evenly
    for f in tun.Faces():
        srf = BRep_Tool.Surface_s(f.wrapped)
        if isinstance(srf, Geom_BSplineSurface):
            u1, u2, v1, v2 = srf.Bounds()
            for k in range(1, 10):
                if srf.VDegree() == 1:
                    srf.InsertVKnot(v1 + (v2 - v1) * k / 10.0, 1, 1e-9, True)
                elif srf.UDegree() == 1:
                    srf.InsertUKnot(u1 + (u2 - u1) * k / 10.0, 1, 1e-9, True)
    return tun


def tilted(shape):
    return shape.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -TILT)


# ------------------------------------------------------------- shell -----
# (everything is first built in the untilted frame: tunnel along -Y, junction
#  section in the plane y = 0; then tilted by TILT about the axle)
dome_w = dome_wire(A_X, B_R, T)
front_w = front_wire(W_F, B_R, N_F, T)

# rolled bead along the front edge: a tube just inside the outer skin (it
# rounds the edge off and stands proud on the inside)
bead_path = cq.Wire.assembleEdges([sup_curve(W_F - BEAD_R - 1.0, B_R - BEAD_R - 1.0, N_F, R_MIN, 17)[0]])
bead = cq.Solid.sweep(cq.Wire.makeCircle(BEAD_R, bead_path.startPoint(), bead_path.tangentAt(0.0)),
                      [], bead_path, makeSolid=True, isFrenet=True).translate(cq.Vector(0, -L_TUN, 0))

skin = sweep(dome_w, REV_END - TILT).fuse(tunnel_loft(front_w, dome_w), glue=True).fuse(bead).clean()

# solid bounded by the mid-wall surface (used to seat the bracket on the
# fender: the bracket is trimmed to it so that it ends inside the wall)
mid_w = dome_wire(A_X - T / 2, B_R - T / 2)
mid_fill = tilted(sweep(mid_w, REV_END - TILT).fuse(
    tunnel_loft(front_wire(W_F - T / 2, B_R - T / 2, N_F), mid_w), glue=True))

# lower edge of the tunnel skirts with the rounded front corner (tunnel frame)
c_mid = (-L_TUN + CORNER_R - CORNER_R / math.sqrt(2), R_TB + CORNER_R - CORNER_R / math.sqrt(2))
tun_cut = (cq.Workplane("YZ")
           .moveTo(-L_TUN - 20, -80)
           .lineTo(Y_S, -80)
           .lineTo(Y_S, R_TB)
           .lineTo(-L_TUN + CORNER_R, R_TB)
           .threePointArc(c_mid, (-L_TUN, R_TB + CORNER_R))
           .lineTo(-L_TUN - 20, R_TB + CORNER_R)
           .close()
           .extrude(400, both=True).val())

# lower edge behind the tunnel (tilted frame): an S-shaped drop past the axle,
# then a straight rear edge
p_s = tilt_pt(Y_S, R_TB)
big = 600.0
s_pts = [(-8.7, 17.9), (5.5, 10.8), (12.5, -1.9), (17.5, -12.6), (24.0, CUT_M * 24.0 + CUT_C)]
rear_cut = (cq.Workplane("YZ")
            .moveTo(-60.0, -20.0)
            .lineTo(*p_s)
            .spline(s_pts, tangents=[(ct, -st), (1.0, CUT_M)], includeCurrent=True)
            .lineTo(big, CUT_M * big + CUT_C)
            .lineTo(big, -big)
            .lineTo(-60.0, -big)
            .close()
            .extrude(400, both=True).val())

shell = tilted(skin).cut(tilted(tun_cut), rear_cut)

# ------------------------------------------------------- inner doubler -----
a_i, b_i = A_X - T, B_R - T
# wide backing plate under the bracket (inside the crown) ...
doubler = tilted(sweep(dome_wire(a_i + 2.0, b_i + 2.0, DB_T + 2.0), 100.0 - TILT, DB_F)).intersect(
    cq.Solid.makeBox(DB_W, 400, 200, cq.Vector(-DB_W / 2, -200, DB_Z)))
# ... and a narrower strap on top of it running down the back of the dome
strap = tilted(sweep(dome_wire(a_i - DB_T + 1.0, b_i - DB_T + 1.0, DB_T + 1.0), 100.0 - TILT)).intersect(
    cq.Solid.makeBox(ST_W, 400, ST_Z0 - ST_Z, cq.Vector(-ST_W / 2, -200, ST_Z)))


# ------------------------------------------------------------ bracket -----
def tray_block(w2, y0, y1, z0, z1, rc, rb):
    """Block with rounded rear corners (rc, plan view) and rounded top edges
    (rb) except along the open front."""
    sk = (cq.Workplane("XY").workplane(offset=z0)
          .moveTo(-w2, y0).lineTo(w2, y0).lineTo(w2, y1 - rc)
          .radiusArc((w2 - rc, y1), -rc)
          .lineTo(-w2 + rc, y1)
          .radiusArc((-w2, y1 - rc), -rc)
          .close())
    return sk.extrude(z1 - z0).faces(">Z").edges("not <Y").fillet(rb).val()


# bent sheet tray = outer block minus the block offset by the sheet thickness
tray = tray_block(PL_W / 2, PL_Y0, PL_Y1, FL_Z, PL_Z, CORNER_PL, BEND_R).cut(
    tray_block(PL_W / 2 - PL_T, PL_Y0 - 5, PL_Y1 - PL_T, FL_Z - 5, PL_Z - PL_T,
               CORNER_PL - PL_T, BEND_R - PL_T))

# notches in the side flanges where they straddle the fender
notch1 = [(16.5, 100.0), (16.5, 140.6), (24.7, 148.0), (40.3, 148.4),
          (45.5, 143.6), (45.5, 100.0)]
notch2 = [(68.8, 100.0), (68.8, 133.6), (82.8, 146.9), (91.8, 144.5),
          (87.7, 110.0), (87.7, 100.0)]
notches = [cq.Workplane("YZ").polyline(pts).close().extrude(8.0)
           .translate((sx * PL_W / 2.0 - 4.0, 0, 0)).val()
           for pts in (notch1, notch2) for sx in (-1, 1)]

# gusset plate under the tray (right-hand side only), resting on the fender
gusset = (cq.Workplane("YZ")
          .polyline([(74.7, PL_Z - PL_T + 0.5), (PL_Y1 - PL_T + 0.5, PL_Z - PL_T + 0.5),
                     (PL_Y1 - PL_T + 0.5, 146.0), (136.0, 80.0)]).close()
          .extrude(PL_T).translate((GUSSET_X - PL_T / 2.0, 0, 0)).val())

# the bracket sits on the fender: trim it where it enters the fender wall
tray = tray.cut(*notches).fuse(gusset).cut(mid_fill)

# -------------------------------------------------------------- holes -----
holes = []


def drill(p, n, length=24.0, d=HOLE_D):
    n = cq.Vector(*n).normalized()
    p = cq.Vector(*p)
    holes.append(cq.Solid.makeCylinder(d / 2.0, length, p - n * (length / 2.0), n))


def r_tun(x, s):
    """outer radius of the (ruled) tunnel at x, s = distance behind the front."""
    w = min(max(s / L_TUN, 0.0), 1.0)
    return (1.0 - w) * r_sup(x) + w * r_of_x(x)


def tunnel_hole(x, s):
    """hole in the tunnel, x across, s = distance behind the front edge."""
    r = r_tun(x, s)
    drdx = (r_tun(x + 0.1, s) - r_tun(x - 0.1, s)) / 0.2
    drill((x,) + tilt_pt(-L_TUN + s, r), (-drdx,) + tilt_pt(0.0, 1.0), 30.0)


def side_hole(y, z, sx):
    """hole in the skirt at side-view position (y, z), side sx = +-1."""
    yu, zu = untilt_pt(y, z)
    if yu < 0:                       # in the tunnel
        sd = yu + L_TUN
        w = min(max(sd / L_TUN, 0.0), 1.0)
        x = sx * ((1.0 - w) * x_sup(zu) + w * x_of_r(zu))
        drdx = (r_tun(x + 0.1, sd) - r_tun(x - 0.1, sd)) / 0.2
        drill((x, y, z), (-drdx,) + tilt_pt(0.0, 1.0), 30.0)
    else:                            # in the dome
        r = math.hypot(y, z)
        x = sx * x_of_r(r)
        drill((x, y, z), (x / A_X ** 2, y / B_R ** 2, z / B_R ** 2))


# hole on the crown near the front edge
tunnel_hole(0.0, 12.0)
# holes along the edges of both skirts (side view positions)
for y, z in ((-87.8, 139.6), (-96.8, 61.0), (-27.2, 33.4), (22.4, -4.3), (123.8, -24.6)):
    for sx in (-1, 1):
        side_hole(y, z, sx)
# rear centre hole
th = math.radians(99.8)
drill((0.0, B_R * math.sin(th), B_R * math.cos(th)), (0.0, math.sin(th), math.cos(th)))
# bracket holes: four at the rear of the plate, four through plate and fender
bolt_holes = [cq.Solid.makeCylinder(HOLE_D / 2.0, 80.0, cq.Vector(x, y, 110.0), cq.Vector(0, 0, 1))
              for y in (144.5, 6.0) for x in (-53.5, -30.5, 30.5, 53.5)]

shell = shell.cut(*holes, *bolt_holes[4:])
tray = tray.cut(*bolt_holes)

part = shell.fuse(doubler, strap, tray).clean()
result = cq.Workplane("XY").add(part)
